import cadquery as cq

# =====================================================================
# Reducer / hose adapter sleeve.
# Axis along +X.  Large socket end at x = 0, small spigot tip at x = L_TOT.
# The spigot is double walled: an outer sleeve and a drafted inner ring
# separated by a deep annular groove, bridged at the bottom by 3 ribs.
# =====================================================================

# ---------------- driving dimensions (mm) ----------------
R1 = 30.0            # large socket outer radius
L1 = 55.6            # large section length (to the shoulder chamfer)
LIP_W = 3.6          # socket mouth band (separate face band at the mouth)
SH_CH = 2.75         # 45 deg chamfer on the shoulder
L_TOT = 106.9        # overall length
R_TIP = 25.53        # spigot outer radius at the tip

# spigot outer profile: concave blend right after the chamfer that runs
# out into a very slight taper towards the tip (one smooth spline)
SPIGOT_PTS = [(60.0, 26.896), (62.5, 26.57), (66.0, 26.301),
              (71.0, 26.098), (78.0, 25.945), (90.0, 25.764)]
SPIGOT_SLOPE0 = 0.226   # radial slope just after the chamfer
SPIGOT_SLOPE1 = 0.0138  # radial slope at the tip (slight taper)

R_SLEEVE_IN = 23.15  # spigot outer sleeve inner radius (annular groove OD)
R_RING_TIP = 19.80   # inner ring outer radius at the tip
R_RING_BASE = 20.9   # inner ring outer radius at groove bottom (draft)
X_GROOVE_BOT = 55.5  # axial position of the groove bottom
R_BORE = 17.35       # through bore radius of the spigot / inner ring

R_SOCKET = 26.5      # large socket bore radius
X_SOCKET_BOT = 52.5  # socket depth (bottom of large bore)

RIB_W = 2.3          # three ribs bridging the bottom of the groove
RIB_H = 3.0          # rib height above the groove bottom
RIB_ANGLES = [0.0, 120.0, 240.0]   # from +Y toward +Z

# revolve seams are turned to low-visibility angles (deg, +Y toward +Z)
OUTER_SEAM = -50.0
CHAMFER_SEAM = 0.0
INNER_SEAM = 130.0
RING_SEAM = -50.0

EXT = 1.0            # overshoot past end faces for clean boolean cuts


def revolve_x(wp, seam_deg):
    """Revolve a closed XY profile (y = radius) a full turn about the X axis
    and rotate the resulting seam to the requested angle."""
    return wp.revolve(360.0, (0, 0, 0), (1, 0, 0)).rotate((0, 0, 0), (1, 0, 0), seam_deg)


def ring_profile(x0, x1, r0, r1):
    """Closed rectangular (x, r) profile."""
    return (
        cq.Workplane("XY")
        .moveTo(x0, r0)
        .lineTo(x0, r1)
        .lineTo(x1, r1)
        .lineTo(x1, r0)
        .close()
    )


# ---------------- outer envelope ----------------
x_ch = L1 + SH_CH
r_ch = R1 - SH_CH

socket_mouth = revolve_x(ring_profile(0.0, LIP_W, 0.0, R1), OUTER_SEAM)
socket_body = revolve_x(ring_profile(LIP_W, L1, 0.0, R1), OUTER_SEAM)

chamfer_part = revolve_x(
    cq.Workplane("XY")
    .moveTo(L1, 0.0)
    .lineTo(L1, R1)
    .lineTo(x_ch, r_ch)
    .lineTo(x_ch, 0.0)
    .close(),
    CHAMFER_SEAM,
)

spigot_part = revolve_x(
    cq.Workplane("XY")
    .moveTo(x_ch, 0.0)
    .lineTo(x_ch, r_ch)
    .spline(
        SPIGOT_PTS + [(L_TOT, R_TIP)],
        tangents=[(1.0, -SPIGOT_SLOPE0), (1.0, -SPIGOT_SLOPE1)],
        includeCurrent=True,
    )
    .lineTo(L_TOT, 0.0)
    .close(),
    OUTER_SEAM,
)

outer = (
    socket_mouth.union(socket_body, clean=False)
    .union(chamfer_part, clean=False)
    .union(spigot_part, clean=False)
)

# ---------------- socket bore + spigot through bore ----------------
mouth_bore = revolve_x(ring_profile(-EXT, LIP_W, 0.0, R_SOCKET), INNER_SEAM)
main_bore = revolve_x(
    cq.Workplane("XY")
    .moveTo(LIP_W, 0.0)
    .lineTo(LIP_W, R_SOCKET)
    .lineTo(X_SOCKET_BOT, R_SOCKET)
    .lineTo(X_SOCKET_BOT, R_BORE)
    .lineTo(L_TOT + EXT, R_BORE)
    .lineTo(L_TOT + EXT, 0.0)
    .close(),
    INNER_SEAM,
)
cavity = mouth_bore.union(main_bore, clean=False)

# ---------------- annular groove in the spigot ----------------
# sleeve bore cylinder minus the drafted inner ring core
ring_slope = (R_RING_BASE - R_RING_TIP) / (L_TOT - X_GROOVE_BOT)
sleeve_bore = revolve_x(
    ring_profile(X_GROOVE_BOT, L_TOT + EXT, 0.0, R_SLEEVE_IN), INNER_SEAM
)
ring_core = revolve_x(
    cq.Workplane("XY")
    .moveTo(X_GROOVE_BOT - EXT, 0.0)
    .lineTo(X_GROOVE_BOT - EXT, R_RING_BASE + ring_slope * EXT)
    .lineTo(L_TOT + EXT, R_RING_TIP - ring_slope * EXT)
    .lineTo(L_TOT + EXT, 0.0)
    .close(),
    RING_SEAM,
)
groove = sleeve_bore.cut(ring_core)

body = outer.cut(cavity, clean=False).cut(groove, clean=False)

# ---------------- ribs bridging the groove bottom ----------------
for a in RIB_ANGLES:
    r0 = R_RING_BASE - 0.6          # sink slightly into the ring
    r1 = R_SLEEVE_IN + 0.6          # and into the sleeve
    rib = (
        cq.Workplane("XY")
        .box(RIB_H + 0.5, r1 - r0, RIB_W)
        .translate((X_GROOVE_BOT + (RIB_H - 0.5) / 2.0, 0.5 * (r0 + r1), 0.0))
        .rotate((0, 0, 0), (1, 0, 0), a)
    )
    body = body.union(rib, clean=False)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
